import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 50.0            # width along X
D = 84.5            # depth along Y (front face at Y=0)
H = 96.8            # height along Z (bottom at Z=0)
TOP_CH = 4.1        # size of the small face at the top, perpendicular to the slope
BACK_Z = 16.4       # height of the rear vertex (slope meets the rear face)
T = 3.5             # wall thickness (sides, floor, rear)
T_FRONT = 2.5       # front wall thickness

# lid opening on the slope (u = distance down the slope from its top edge)
TAB_U = 3.7         # opening reaches this far up between the screw bosses
BOSS_U = 15.0       # opening starts here beside the bosses
TAB_HALF = 9.9      # half width of the central tab of the opening
BOSS_R = 5.2        # rounding of the boss corners

# lid screw holes (perpendicular to slope, exit on the front face)
LID_HOLE_X = 15.7
LID_HOLE_U = 9.5
LID_HOLE_D = 5.7
LID_CB_D = 8.6
LID_CB_DEPTH = 11.8

# nut-trap side slots
SLOT_Y0, SLOT_Y1 = 14.1, 37.4
SLOT_Z0, SLOT_Z1 = 14.3, 26.1
SLOT_TIP = 4.5      # length of the pointed end along Y
SLOT_FLAT = 4.15    # flat at the tip
HOUSE_TOP_Z = 29.2  # top of the nut housings
HOUSE_SLANT_Y = 34.5   # where the top of the housing starts to slope down
HOUSE_TIP_Y = 40.15    # rear tip of the housing
HOUSE_TIP_H = 7.6      # height of the flat rear tip
HOUSE_L_X = (-21.5, -1.4)   # left housing X range (inside the cavity)
HOUSE_R_X = (12.5, 21.5)    # right housing X range
BOT_HOLE_D = 5.5
BOT_HOLE_X = (-7.9, 18.4)
BOT_HOLE_Y = 23.9

# vent slots
N_VENT = 6
VENT_PITCH = 5.66
VENT_W = 2.9
FLOOR_VENT_Y = (35.6, 65.6)
BACK_VENT_W0, BACK_VENT_W1 = 1.7, 13.0   # along inner back wall from the floor
VENT_R = 0.6        # corner radius of the vent slots

# groove across the inside of the rear wall (catch for the lid)
GROOVE_Z0, GROOVE_Z1 = 14.75, 17.35
GROOVE_BACK_Y = 80.8

# thumb wheel: three thin discs on a common hub (axis along Y)
DISC_R = 14.4
DISC_Z = 48.3
DISC_PLATES = [(38.6, 1.3), (40.75, 0.8), (42.7, 1.8)]   # (front Y, thickness)
HUB_D = 4.0
REAR_GROOVE_W = 0.8     # groove round the rim of the rear disc
REAR_GROOVE_D = 0.5

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived geometry ----------------
S2 = math.sqrt(2.0)
SLOPE_C = H + TOP_CH          # slope plane: Z = SLOPE_C - Y
BACK_C = BACK_Z - D           # rear face: Z = Y + BACK_C
Y_BOT_BACK = -BACK_C          # where rear face meets the floor
P0 = cq.Vector(0, TOP_CH, H)  # top edge of the slope
NRM = cq.Vector(0, 1, 1).normalized()      # outward normal of slope
DWN = cq.Vector(0, 1, -1).normalized()     # down the slope
L_SLOPE = (D - TOP_CH) * S2


def yz_prism(pts, x0, x1):
    """Extrude a closed polygon given in (Y, Z) along X from x0 to x1."""
    wp = cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close()
    return wp.extrude(x1 - x0)


def slope_plane(offset=0.0):
    return cq.Plane(origin=P0 + NRM * offset, xDir=(1, 0, 0), normal=NRM.toTuple())


# ---------------- outer wedge ----------------
outer_pts = [
    (0, 0),
    (0, H - TOP_CH),
    (TOP_CH, H),
    (D, BACK_Z),
    (Y_BOT_BACK, 0),
]
body = yz_prism(outer_pts, -W / 2, W / 2)

# ---------------- cavity ----------------
BIG = 300.0
ci = BACK_C + T * S2          # inner rear wall: Z = Y + ci
inner_pts = [
    (T_FRONT, T),
    (T - ci, T),               # floor meets inner rear wall
    (BIG - ci, BIG),
    (T_FRONT, BIG),
]
inner = yz_prism(inner_pts, -W / 2 + T, W / 2 - T)

# opening outline on the slope, as a prism perpendicular to it
# local coords of the slope plane: x = X, y = u (down the slope)
u_end = L_SLOPE + 50
xi = W / 2 - T
R = BOSS_R
pl = slope_plane(20.0)
opening = (
    cq.Workplane(pl)
    .moveTo(-xi, u_end)
    .lineTo(-xi, BOSS_U)
    .lineTo(-TAB_HALF - R, BOSS_U)
    .threePointArc(
        (-TAB_HALF - R + R * math.sin(math.pi / 4), BOSS_U - R + R * math.cos(math.pi / 4)),
        (-TAB_HALF, BOSS_U - R),
    )
    .lineTo(-TAB_HALF, TAB_U)
    .lineTo(TAB_HALF, TAB_U)
    .lineTo(TAB_HALF, BOSS_U - R)
    .threePointArc(
        (TAB_HALF + R - R * math.sin(math.pi / 4), BOSS_U - R + R * math.cos(math.pi / 4)),
        (TAB_HALF + R, BOSS_U),
    )
    .lineTo(xi, BOSS_U)
    .lineTo(xi, u_end)
    .close()
    .extrude(-150)
)

cavity = inner.intersect(opening)
body = body.cut(cavity)

# ---------------- nut housings ----------------
zmid = (SLOT_Z0 + SLOT_Z1) / 2
zbot_h = 2 * zmid - HOUSE_TOP_Z
house_pts = [
    (T_FRONT - 0.5, T - 0.5),
    (T_FRONT - 0.5, HOUSE_TOP_Z),
    (HOUSE_SLANT_Y, HOUSE_TOP_Z),
    (HOUSE_TIP_Y, zmid + HOUSE_TIP_H / 2),
    (HOUSE_TIP_Y, zmid - HOUSE_TIP_H / 2),
    (HOUSE_SLANT_Y, zbot_h),
    (HOUSE_SLANT_Y, T - 0.5),
]
house_l = yz_prism(house_pts, HOUSE_L_X[0] - 0.5, HOUSE_L_X[1])
house_r = yz_prism(house_pts, HOUSE_R_X[0], HOUSE_R_X[1] + 0.5)
body = body.union(house_l).union(house_r)

# side slots (through both walls and both housings)
slot_pts = [
    (SLOT_Y0, SLOT_Z0),
    (SLOT_Y0, SLOT_Z1),
    (SLOT_Y1 - SLOT_TIP, SLOT_Z1),
    (SLOT_Y1, zmid + SLOT_FLAT / 2),
    (SLOT_Y1, zmid - SLOT_FLAT / 2),
    (SLOT_Y1 - SLOT_TIP, SLOT_Z0),
]
body = body.cut(yz_prism(slot_pts, -W / 2 - 1, W / 2 + 1))

# screw holes from the bottom into the slots
for hx in BOT_HOLE_X:
    h = (
        cq.Workplane("XY", origin=(hx, BOT_HOLE_Y, -1))
        .circle(BOT_HOLE_D / 2)
        .extrude(SLOT_Z0 + 2)
    )
    body = body.cut(h)

# ---------------- rear groove ----------------
groove = (
    cq.Workplane("XY")
    .box(W - 2 * T, 15.0, GROOVE_Z1 - GROOVE_Z0, centered=(True, False, False))
    .translate((0, GROOVE_BACK_Y - 15.0, GROOVE_Z0))
)
body = body.cut(groove)


def vent_sketch(w, l):
    return cq.Sketch().rect(w, l).vertices().fillet(VENT_R)


# ---------------- floor vents ----------------
vx = [(i - (N_VENT - 1) / 2) * VENT_PITCH for i in range(N_VENT)]
fl = FLOOR_VENT_Y[1] - FLOOR_VENT_Y[0]
for x in vx:
    v = (
        cq.Workplane("XY", origin=(x, (FLOOR_VENT_Y[0] + FLOOR_VENT_Y[1]) / 2, -1))
        .placeSketch(vent_sketch(VENT_W, fl))
        .extrude(T + 2)
    )
    body = body.cut(v)

# ---------------- rear wall vents ----------------
# rear wall inner face passes through (T - ci, T) along direction (1,1)/sqrt2
corner = cq.Vector(0, T - ci, T)
wall_dir = cq.Vector(0, 1, 1).normalized()
wall_nrm = cq.Vector(0, 1, -1).normalized()   # outward normal of rear wall
wc = (BACK_VENT_W0 + BACK_VENT_W1) / 2
wl = BACK_VENT_W1 - BACK_VENT_W0
for x in vx:
    org = corner + wall_dir * wc + cq.Vector(x, 0, 0) - wall_nrm * 1.0
    plw = cq.Plane(origin=org.toTuple(), xDir=(1, 0, 0), normal=wall_nrm.toTuple())
    v = cq.Workplane(plw).placeSketch(vent_sketch(VENT_W, wl)).extrude(T + 2)
    body = body.cut(v)

# ---------------- lid screw holes ----------------
for sx in (-LID_HOLE_X, LID_HOLE_X):
    pt = P0 + DWN * LID_HOLE_U + cq.Vector(sx, 0, 0)
    plh = cq.Plane(origin=(pt + NRM * 1.0).toTuple(), xDir=(1, 0, 0), normal=(-NRM).toTuple())
    hole = cq.Workplane(plh).circle(LID_HOLE_D / 2).extrude(40)
    body = body.cut(hole)
    # counterbore from the front face along the same axis
    # axis hits Y=0 at distance pt.y*sqrt2 from pt
    dist = pt.y * S2
    exit_pt = pt - NRM * dist
    plc = cq.Plane(origin=(exit_pt - NRM * 5).toTuple(), xDir=(1, 0, 0), normal=NRM.toTuple())
    cb = cq.Workplane(plc).circle(LID_CB_D / 2).extrude(5 + LID_CB_DEPTH)
    body = body.cut(cb)

# ---------------- thumb wheel ----------------
y_front = DISC_PLATES[0][0]
y_back = DISC_PLATES[-1][0] + DISC_PLATES[-1][1]
disc = (
    cq.Workplane("XZ", origin=(0, y_back, DISC_Z))
    .circle(HUB_D / 2)
    .extrude(y_back - y_front)
)
for i, (py, pt_) in enumerate(DISC_PLATES):
    if i == len(DISC_PLATES) - 1:
        # rear disc with a groove round its rim (revolved profile, r along X)
        a = (pt_ - REAR_GROOVE_W) / 2
        prof = [
            (0, py),
            (DISC_R, py),
            (DISC_R, py + a),
            (DISC_R - REAR_GROOVE_D, py + a),
            (DISC_R - REAR_GROOVE_D, py + pt_ - a),
            (DISC_R, py + pt_ - a),
            (DISC_R, py + pt_),
            (0, py + pt_),
        ]
        plate = (
            cq.Workplane("XY")
            .polyline(prof)
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
            .translate((0, 0, DISC_Z))
        )
    else:
        plate = (
            cq.Workplane("XZ", origin=(0, py + pt_, DISC_Z))
            .circle(DISC_R)
            .extrude(pt_)
        )
    disc = disc.union(plate)

result = body.union(disc)
